import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
N_BLOCKS = 5          # terminal blocks in the strip (along Y)
H = 20.0              # block height (Z)
W = 19.0              # block width (X)
L = 34.0              # block length (Y)
GAP = 1.6             # gap between neighbouring blocks

SLOT = 1.8            # central through slot between the two halves
CAV_HALF = 4.34       # half width of the H shaped channel
CAV_BAND = 4.2        # height of the channel's middle band
CAV_LEG_W = 1.8       # width of the channel's tall outer parts
CAV_LEG_H = 7.6       # height of the tall outer parts
LEDGE_BEVEL = 0.65    # bevel on the channel ledges at the block ends

RIM_OUT = 1.5         # outer wall thickness around the top wire entries
RIM_IN = 1.0          # wall thickness on the slot side
RIM_END = 1.5         # wall thickness at the block ends
POCKET_D = 6.0        # depth of the top wire entries

# screws (on +X and -X faces, centre of block)
SCREW_HEAD_D = 7.1
SCREW_HEAD_T = 1.7
SCREW_NECK_D = 4.9
SCREW_NECK_L = 1.55
SCREW_SLOT_W = 1.5
SCREW_SLOT_D = 1.2
SCREW_CHAMF = 0.75

# pins (small round bosses next to each screw)
PIN_D = 4.7
PIN_H = 2.3
PIN_CHAMF = 0.5
PIN_Y = (0.14, 0.76)  # fractions of L on the +X face (mirrored by 180deg on -X)

# notch at the +X/+Y and -X/-Y corners of every block
NOTCH_Y = 3.2         # notch length along Y
NOTCH_H = 7.6         # notch height
NOTCH_X = 0.6         # shallow outer part depth
# waist shaped recess seen on the end faces (u = inward from side wall, v = half height)
WAIST = [(0.0, 2.74), (1.76, 2.02), (2.58, 2.02), (4.24, 2.64), (5.17, 2.53)]
WAIST_ARC1_MID = (0.95, 2.52)   # through-points of the two curved flanks
WAIST_ARC2_MID = (3.4, 2.5)

# bottom texture
GROOVES_X = 8         # groove rows across the bottom per block
GROOVE_W = 1.2
GROOVE_D = 1.4
SLOTS_END = ((-1.0, 2.76), (3.5, 5.05), (5.88, 9.5))   # slot spans at the block ends
SLOTS_MID = ((-1.0, 1.4), (3.5, 5.05), (7.2, 9.5))     # slot spans in the interior rows
CROSS_U = (4.28,)      # centres of the cross arms (u from side wall)
CROSS_W = 0.8
CROSS_L = 2.6

# jumper bar
ROD_D = 3.8
ROD_Z = 3.55          # rod centre above block top
STAPLE_W = 7.3        # overall width of each U bridge (X)
STAPLE_T = 3.6        # thickness of each U bridge (Y)
STAPLE_TOP = 5.3      # bridge top above block top
STAPLE_GAP_TOP = 2.2  # top of the opening under the bridge, above block top
STAPLE_CORNER = 1.6   # outer corner radius of the U
STAPLE_FILLET = 1.36  # rounding of the U edges (makes the wire read as round)
LEG_Y = 0.953         # bridge position (fraction of L)
LEG_SINK = 0.3        # how far the legs reach into the block


def waist_profile(sign):
    """Closed waist outline in the XZ plane for the half on side `sign` (+1 = +X)."""
    zc = H / 2.0
    x0 = sign * W / 2.0
    top = [(x0 - sign * u, zc + v) for (u, v) in WAIST]
    bot = [(x0 - sign * u, zc - v) for (u, v) in WAIST]
    uin = WAIST[-1][0] + 0.3
    wp = cq.Workplane("XZ").moveTo(x0 + sign * 0.5, zc + WAIST[0][1])
    wp = wp.lineTo(*top[0])
    wp = wp.threePointArc((x0 - sign * WAIST_ARC1_MID[0], zc + WAIST_ARC1_MID[1]), top[1])
    wp = wp.lineTo(*top[2])
    wp = wp.threePointArc((x0 - sign * WAIST_ARC2_MID[0], zc + WAIST_ARC2_MID[1]), top[3])
    wp = wp.lineTo(x0 - sign * uin, zc + WAIST[-1][1])
    wp = wp.lineTo(x0 - sign * uin, zc - WAIST[-1][1])
    wp = wp.lineTo(*bot[3])
    wp = wp.threePointArc((x0 - sign * WAIST_ARC2_MID[0], zc - WAIST_ARC2_MID[1]), bot[2])
    wp = wp.lineTo(*bot[1])
    wp = wp.threePointArc((x0 - sign * WAIST_ARC1_MID[0], zc - WAIST_ARC1_MID[1]), bot[0])
    wp = wp.lineTo(x0 + sign * 0.5, zc - WAIST[0][1])
    wp = wp.close()
    return wp


def block():
    """One terminal block, local coords x in [-W/2, W/2], y in [0, L], z in [0, H]."""
    zc = H / 2.0
    b = cq.Workplane("XY").box(W, L, H, centered=(True, False, False))

    # central through slot (full height, full length)
    slot = cq.Workplane("XY").box(SLOT, L + 2, H + 2, centered=(True, False, False)).translate((0, -1, -1))
    b = b.cut(slot)

    # H shaped channel running along Y
    cav = cq.Workplane("XY").box(2 * CAV_HALF, L + 2, CAV_BAND).translate((0, L / 2, zc))
    for s in (-1, 1):
        leg = cq.Workplane("XY").box(CAV_LEG_W, L + 2, CAV_LEG_H).translate(
            (s * (CAV_HALF - CAV_LEG_W / 2), L / 2, zc))
        cav = cav.union(leg)
    b = b.cut(cav)

    # small bevels on the channel ledges at both block ends
    xl = CAV_HALF - CAV_LEG_W
    e = 0.02
    for (ye, d) in ((0.0, 1.0), (L, -1.0)):
        for t in (-1.0, 1.0):
            zb = zc + t * CAV_BAND / 2
            pts = [(ye - d * e, zb - t * e), (ye - d * e, zb + t * (LEDGE_BEVEL + e)),
                   (ye + d * (LEDGE_BEVEL + e), zb - t * e)]
            wedge = (cq.Workplane("YZ").workplane(offset=-xl).polyline(pts).close()
                     .extrude(2 * xl))
            b = b.cut(wedge)

    # top wire entries (one per half)
    pw = W / 2 - SLOT / 2 - RIM_OUT - RIM_IN
    pl = L - 2 * RIM_END
    for s in (-1, 1):
        xc = s * (SLOT / 2 + RIM_IN + pw / 2)
        pk = cq.Workplane("XY").box(pw, pl, POCKET_D + 1).translate(
            (xc, L / 2, H - POCKET_D + (POCKET_D + 1) / 2))
        b = b.cut(pk)

    # bottom texture: rows of short slots (u = distance in from the side wall);
    # the rows at the block ends are longer, interior rows are short pockets
    pitch = L / GROOVES_X
    half = W / 2 - SLOT / 2
    gsolids = []
    for i in range(GROOVES_X + 1):
        y = i * pitch
        segs = SLOTS_END if i in (0, GROOVES_X) else SLOTS_MID
        for s in (-1, 1):
            for (u0, u1) in segs:
                u1 = min(u1, half + 0.5)
                xa = s * (W / 2 - u0)
                xb = s * (W / 2 - u1)
                gsolids.append(cq.Solid.makeBox(abs(xb - xa), GROOVE_W, 2 * GROOVE_D,
                                                cq.Vector(min(xa, xb), y - GROOVE_W / 2, -GROOVE_D)))
    b = b.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(gsolids)))
    # short cross arms along Y through the interior pockets (separate pass: tools must not overlap)
    gsolids = []
    for i in range(1, GROOVES_X):
        y = i * pitch
        for s in (-1, 1):
            for uc in CROSS_U:
                xc = s * (W / 2 - uc)
                gsolids.append(cq.Solid.makeBox(CROSS_W, CROSS_L, 2 * GROOVE_D,
                                                cq.Vector(xc - CROSS_W / 2, y - CROSS_L / 2, -GROOVE_D)))
    b = b.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(gsolids)))

    # corner notches (+X,+Y) and (-X,-Y): shallow outer notch + waist recess
    for s in (-1, 1):
        yc = L - NOTCH_Y / 2 if s > 0 else NOTCH_Y / 2
        n = cq.Workplane("XY").box(2 * NOTCH_X, NOTCH_Y + 0.02, NOTCH_H).translate(
            (s * W / 2, yc + s * 0.01, zc))
        b = b.cut(n)
        wz = waist_profile(s).extrude(NOTCH_Y + 0.02)   # XZ workplane extrudes towards -Y
        if s > 0:
            wz = wz.translate((0, L + 0.01, 0))
        else:
            wz = wz.translate((0, NOTCH_Y + 0.01 - 0.02, 0))
        b = b.cut(wz)

    # screws and pins on both side faces (block is 180deg symmetric about Z)
    for s in (-1, 1):
        yS = L / 2
        x0 = s * W / 2
        neck = (cq.Workplane("YZ").circle(SCREW_NECK_D / 2)
                .extrude(SCREW_NECK_L + SCREW_HEAD_T / 2)
                .translate((-0.2, yS, zc)))
        head = (cq.Workplane("YZ").circle(SCREW_HEAD_D / 2).extrude(SCREW_HEAD_T)
                .faces(">X").edges().chamfer(SCREW_CHAMF)
                .translate((SCREW_NECK_L, yS, zc)))
        screw = neck.union(head)
        cut_slot = cq.Workplane("XY").box(SCREW_SLOT_D * 2, SCREW_HEAD_D + 2, SCREW_SLOT_W).translate(
            (SCREW_NECK_L + SCREW_HEAD_T, yS, zc))
        screw = screw.cut(cut_slot)
        if s < 0:
            screw = screw.mirror("YZ", basePointVector=(0, 0, 0))
        screw = screw.translate((x0, 0, 0))
        b = b.union(screw)

        for f in PIN_Y:
            y = f * L if s > 0 else (1 - f) * L
            pin = (cq.Workplane("YZ").circle(PIN_D / 2).extrude(PIN_H + 0.2)
                   .faces(">X").edges().chamfer(PIN_CHAMF)
                   .translate((-0.2, y, zc)))
            if s < 0:
                pin = pin.mirror("YZ", basePointVector=(0, 0, 0))
            pin = pin.translate((x0, 0, 0))
            b = b.union(pin)
    return b


def staple(yc):
    """Inverted U bridge of rounded wire straddling the slot at Y = yc."""
    A = STAPLE_W / 2
    gi = SLOT / 2
    zt = H + STAPLE_TOP
    zi = H + STAPLE_GAP_TOP
    z0 = H - LEG_SINK
    rc = STAPLE_CORNER
    wp = (cq.Workplane("XZ").moveTo(-A, z0).lineTo(-A, zt - rc)
          .radiusArc((-A + rc, zt), rc).lineTo(A - rc, zt).radiusArc((A, zt - rc), rc)
          .lineTo(A, z0).lineTo(gi, z0).lineTo(gi, zi).lineTo(-gi, zi).lineTo(-gi, z0).close())
    s = wp.extrude(STAPLE_T / 2, both=True)
    # round off the edges so legs and top run read as round wire
    s = s.faces("<Y or >Y").edges("not(<Z)").fillet(STAPLE_FILLET)
    return s.translate((0, yc, 0))


pitch_y = L + GAP
blk = block()
parts = blk
for i in range(1, N_BLOCKS):
    parts = parts.union(blk.translate((0, i * pitch_y, 0)))

# jumper bar: one U bridge per block + rod along the centre line
leg_ys = [i * pitch_y + LEG_Y * L for i in range(N_BLOCKS)]
for y in leg_ys:
    parts = parts.union(staple(y))
rod_len = leg_ys[-1] - leg_ys[0]
rod = (cq.Workplane("XZ").circle(ROD_D / 2).extrude(-rod_len)
       .translate((0, leg_ys[0], H + ROD_Z)))
parts = parts.union(rod)

# centre the strip on the origin in X/Y
total = N_BLOCKS * L + (N_BLOCKS - 1) * GAP
result = parts.translate((0, -total / 2, 0))
